import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
W = 153.0          # width of the front channel block (X)
H = 205.0          # height of the front channel block (Z)
D = 57.0           # depth of the flanges (Y)
TF = 31.0          # flange thickness
TW = 14.0          # web thickness (web sits at the back of the flanges)
TP = 22.0          # thickness of the twisted top / bottom plates
Y_RW = 247.0       # front face of the rear wall
T_RW = 13.0        # rear wall thickness
TA = 12.0          # thickness of the rear arms
TWIST = 15.0       # rotation of the rear section about the Y axis (deg)
RW_FIL = 5.0       # fillet between rear wall back face and the arms
ZC = H / 2.0       # twist axis height

# top arm (round end with bolt circle)
TOP_END_Y = 399.5
TOP_END_R = 59.2
BC_R = 35.0
BC_N = 8
BC_D = 10.0

# bottom arm (lug)
LUG_Y = 400.0
LUG_R = 35.0
LUG_HOLE = 38.0

# flange holes
FH_D = 10.0
FH_PTS = [(-35.0, 33.0), (35.0, 33.0), (-58.5, 9.0), (58.5, 9.0)]

# top flange groove (underside, open to the front)
GR_W = 95.0
GR_H = 13.0
GR_D = 20.0
GR_R = 4.0         # ceiling edge fillets

# bottom flange pockets (top side, open to the front)
PK_W = 32.5
PK_H = 12.5
PK_D = 18.0
PK_X = 31.25
PK_R = 4.0         # vertical back corners
PK_RIM = 1.5       # rim fillet of the pockets


def rot_pt(x, y, z, ang=TWIST):
    a = math.radians(ang)
    dz = z - ZC
    return (x * math.cos(a) + dz * math.sin(a), y,
            -x * math.sin(a) + dz * math.cos(a) + ZC)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------------------------------------------------------- front block
top_flange = box(-W / 2, W / 2, 0, D, H - TF, H)
bot_flange = box(-W / 2, W / 2, 0, D, 0, TF)
web = box(-W / 2, W / 2, D - TW, D, 0, H)
block = top_flange.union(bot_flange).union(web)

# groove in the underside of the top flange
groove = (box(-GR_W / 2, GR_W / 2, -5, GR_D, H - TF - 5, H - TF + GR_H)
          .faces(">Z").edges().fillet(GR_R))
block = block.cut(groove)

# pockets in the top of the bottom flange
for sx in (-1, 1):
    pk = (box(sx * PK_X - PK_W / 2, sx * PK_X + PK_W / 2, -5, PK_D,
              TF - PK_H, TF + 5)
          .edges("|Z and >Y").fillet(PK_R))
    block = block.cut(pk)
    # soften the rim of the pocket where it breaks the flange top face
    x0, x1 = sx * PK_X - PK_W / 2, sx * PK_X + PK_W / 2
    try:
        block = block.edges(cq.selectors.BoxSelector(
            (x0 - 1.0, 0.5, TF - 0.2), (x1 + 1.0, PK_D + 1.0, TF + 0.2))).fillet(PK_RIM)
    except Exception:
        pass

# flange holes
for (hx, hy) in FH_PTS:
    cyl = (cq.Workplane("XY").workplane(offset=-1).center(hx, hy)
           .circle(FH_D / 2).extrude(H + 2))
    block = block.cut(cyl)


# ---------------------------------------------------------------- twisted plates
# The plates between the front block and the rear wall twist linearly from 0 to
# TWIST degrees.  They are ruled lofts between the straight front section and the
# rotated rear section (bilinear surfaces); the loft also passes through the exact
# mid section and the wires carry a vertex at mid-width so each twisted face is a
# 2 x 2 patchwork of the same bilinear surface.
TW_SEG = 2


def lerp(p, q, s):
    return tuple(a + (b - a) * s for a, b in zip(p, q))


def twisted_plate(z0, z1):
    pts0 = [(-W / 2, D, z0), (0.0, D, z0), (W / 2, D, z0),
            (W / 2, D, z1), (0.0, D, z1), (-W / 2, D, z1)]
    pts1 = [rot_pt(x, Y_RW, z) for (x, _, z) in pts0]
    wires = []
    for i in range(TW_SEG + 1):
        s = i / TW_SEG
        pts = [lerp(p, q, s) for p, q in zip(pts0, pts1)]
        wires.append(cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True))
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, True))


tw_top = twisted_plate(H - TP, H)
tw_bot = twisted_plate(0, TP)


# ---------------------------------------------------------------- rear section (built un-rotated)
def tangent_points(px, py, cx, cy, r):
    dx, dy = px - cx, py - cy
    d = math.hypot(dx, dy)
    base = math.atan2(dy, dx)
    off = math.acos(r / d)
    return [(cx + r * math.cos(base + s * off), cy + r * math.sin(base + s * off))
            for s in (1, -1)]


def arm_outline(z0, t, yc, r):
    y0 = Y_RW
    y1 = Y_RW + T_RW
    tr = max(tangent_points(W / 2, y1, 0.0, yc, r), key=lambda p: p[0])
    tl = min(tangent_points(-W / 2, y1, 0.0, yc, r), key=lambda p: p[0])
    wp = (cq.Workplane("XY").workplane(offset=z0)
          .moveTo(-W / 2, y0).lineTo(W / 2, y0).lineTo(W / 2, y1)
          .lineTo(tr[0], tr[1])
          .threePointArc((0.0, yc + r), (tl[0], tl[1]))
          .lineTo(-W / 2, y1).close())
    return wp.extrude(t)


top_arm = arm_outline(H - TA, TA, TOP_END_Y, TOP_END_R)
for k in range(BC_N):
    a = 2 * math.pi * k / BC_N
    cyl = (cq.Workplane("XY").workplane(offset=H - TA - 1)
           .center(BC_R * math.cos(a), TOP_END_Y + BC_R * math.sin(a))
           .circle(BC_D / 2).extrude(TA + 2))
    top_arm = top_arm.cut(cyl)

bot_arm = arm_outline(0.0, TA, LUG_Y, LUG_R)
bot_arm = bot_arm.cut(cq.Workplane("XY").workplane(offset=-1)
                      .center(0, LUG_Y).circle(LUG_HOLE / 2).extrude(TA + 2))

rear_wall = box(-W / 2, W / 2, Y_RW, Y_RW + T_RW, 0, H)

rear = rear_wall.union(top_arm).union(bot_arm)
# fillets where the back face of the rear wall meets the two arms
y_back = Y_RW + T_RW
for z_j in (H - TA, TA):
    rear = rear.edges(cq.selectors.BoxSelector(
        (-W, y_back - 0.5, z_j - 0.5), (W, y_back + 0.5, z_j + 0.5))).fillet(RW_FIL)
rear = rear.rotate((0, 0, ZC), (0, 1, ZC), TWIST)

# ---------------------------------------------------------------- assemble
body = block.union(tw_top).union(tw_bot).union(rear)

# ---------------------------------------------------------------- engraved part number
TXT = "4202"
TXT_SIZE = 19.0
TXT_FONT = "DejaVu Serif"
TXT_DEPTH = 1.0
TXT_Z = 108.0       # height of the text centre on the web
TXT_Z_BACK = ZC     # height of the text centre on the rear wall (un-rotated)
try:
    txt_front = (cq.Workplane(cq.Plane(origin=(0, D - TW, TXT_Z),
                                       xDir=(1, 0, 0), normal=(0, -1, 0)))
                 .transformed(rotate=(0, 0, -90))
                 .text(TXT, TXT_SIZE, -TXT_DEPTH, combine=False, font=TXT_FONT))
    body = body.cut(txt_front)
    txt_back = (cq.Workplane(cq.Plane(origin=(0, Y_RW + T_RW, TXT_Z_BACK),
                                      xDir=(-1, 0, 0), normal=(0, 1, 0)))
                .transformed(rotate=(0, 0, 90))
                .text(TXT, TXT_SIZE, -TXT_DEPTH, combine=False, font=TXT_FONT))
    txt_back = txt_back.rotate((0, 0, ZC), (0, 1, ZC), TWIST)
    body = body.cut(txt_back)
except Exception:
    pass

result = body

VIEW = {"azimuth": 45, "elevation": 26}
